import cadquery as cq

# ---------------- driving dimensions (mm) ----------------
PLATE_L = 150.0      # base plate length (X)
PLATE_W = 99.3       # base plate width  (Y)
PLATE_T = 6.2        # base plate thickness

BLOCK_L = 143.4      # raised block length (X)
BLOCK_W = 66.1       # raised block width  (Y)
BLOCK_H = 19.8       # raised block height above plate
BLOCK_R = 6.5        # vertical corner radius of block

P1_L, P1_W, P1_R = 126.2, 48.6, 7.3     # main pocket
P1_DEPTH = 11.0                          # main pocket depth from top

P2_L, P2_W, P2_R = 115.2, 46.0, 11.8    # outer outline of groove
P3_L, P3_W, P3_R = 100.4, 30.7, 5.3     # island inside the groove
GROOVE_DEPTH = 5.0                       # groove depth below main pocket floor

RECT_L, RECT_W = 83.8, 28.6              # shallow nest in island top
RECT_DEPTH = 1.2

TAB_L, TAB_W = 6.6, 8.5                  # small tabs at nest ends
TAB_DEPTH = 0.15

# plate holes
BIG_HOLE_D = 7.6
BIG_HOLE_X = 69.7
SMALL_HOLE_D = 5.0
SMALL_HOLE_X = 58.0
HOLE_Y = 42.2
HEX_AF = 8.0          # hex nut pocket (from below) across flats
HEX_DEPTH = 3.0

# vent / port at +X end
PORT_X = 67.3
PORT_D = 5.0
CHAN_W = 6.5          # channel from pocket wall to port (Y width)
CHAN_H = 2.0          # channel height above pocket floor

# ---------------- derived ----------------
Z_TOP = PLATE_T + BLOCK_H
Z_P1 = Z_TOP - P1_DEPTH
Z_GROOVE = Z_P1 - GROOVE_DEPTH
Z_ISLAND = Z_P1               # island top is flush with the pocket floor

# base plate
plate = cq.Workplane("XY").box(PLATE_L, PLATE_W, PLATE_T, centered=(True, True, False))

# raised block
block = (
    cq.Workplane("XY").workplane(offset=PLATE_T)
    .sketch().rect(BLOCK_L, BLOCK_W).vertices().fillet(BLOCK_R).finalize()
    .extrude(BLOCK_H)
)
body = plate.union(block)

# main pocket
p1 = (
    cq.Workplane("XY").workplane(offset=Z_P1)
    .sketch().rect(P1_L, P1_W).vertices().fillet(P1_R).finalize()
    .extrude(P1_DEPTH + 1.0)
)
body = body.cut(p1)

# groove around the island
groove_outer = (
    cq.Workplane("XY").workplane(offset=Z_GROOVE)
    .sketch().rect(P2_L, P2_W).vertices().fillet(P2_R).finalize()
    .extrude(GROOVE_DEPTH + 0.5)
)
island = (
    cq.Workplane("XY").workplane(offset=Z_GROOVE - 1.0)
    .sketch().rect(P3_L, P3_W).vertices().fillet(P3_R).finalize()
    .extrude(GROOVE_DEPTH + 3.0)
)
body = body.cut(groove_outer.cut(island))

# shallow nest in island top
nest = (
    cq.Workplane("XY").workplane(offset=Z_ISLAND - RECT_DEPTH)
    .rect(RECT_L, RECT_W).extrude(RECT_DEPTH + 1.0)
)
body = body.cut(nest)

# end tabs of the nest
for sx in (-1, 1):
    tab = (
        cq.Workplane("XY").workplane(offset=Z_ISLAND - TAB_DEPTH)
        .center(sx * (RECT_L / 2 + TAB_L / 2 - 0.5), 0)
        .rect(TAB_L + 1.0, TAB_W).extrude(TAB_DEPTH + 1.0)
    )
    body = body.cut(tab)

# plate holes
big_pts = [(sx * BIG_HOLE_X, sy * HOLE_Y) for sx in (-1, 1) for sy in (-1, 1)]
small_pts = [(sx * SMALL_HOLE_X, sy * HOLE_Y) for sx in (-1, 1) for sy in (-1, 1)]
big_holes = (
    cq.Workplane("XY").workplane(offset=-1.0)
    .pushPoints(big_pts).circle(BIG_HOLE_D / 2).extrude(PLATE_T + 2.0)
)
small_holes = (
    cq.Workplane("XY").workplane(offset=-1.0)
    .pushPoints(small_pts).circle(SMALL_HOLE_D / 2).extrude(PLATE_T + 2.0)
)
body = body.cut(big_holes).cut(small_holes)
hex_d = HEX_AF / 0.8660254
hexes = (
    cq.Workplane("XY").workplane(offset=-0.5)
    .pushPoints(small_pts).polygon(6, hex_d).extrude(HEX_DEPTH + 0.5)
)
body = body.cut(hexes)

# vertical port in the +X rim, joined to the pocket by a channel at floor level
port = (
    cq.Workplane("XY").workplane(offset=Z_P1)
    .center(PORT_X, 0).circle(PORT_D / 2).extrude(P1_DEPTH + 1.0)
)
body = body.cut(port)
chan_x0 = P1_L / 2 - 1.0
chan_x1 = PORT_X + PORT_D / 2 + 0.8
chan = (
    cq.Workplane("XY").workplane(offset=Z_P1)
    .center((chan_x0 + chan_x1) / 2, 0)
    .rect(chan_x1 - chan_x0, CHAN_W).extrude(CHAN_H)
)
body = body.cut(chan)

result = body
